import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
PITCH = 19.05          # key spacing (rows)
COL_PITCH = 18.93      # column spacing
HOLE = 14.0            # switch cut-out
PLATE_T = 1.2          # top plate thickness
EDGE_R_BOT = 0.8       # rounded lower edge of the plate outline
RIB_W = 1.6            # width of the grid ribs under the plate
RIB_D = 4.7            # ribs reach this depth below the top surface
POST_D = 2.4           # support post diameter
POST_L = 15.8          # posts reach this depth below the top surface
HULL_GAP = 5.0         # neighbouring corner posts closer than this are joined by a web
WEB_L = 13.8           # webs stop a little above the post ends
STANDOFF_D = 8.5
STANDOFF_L = 12.7
STANDOFF_HOLE = 3.0
PIN_COLLAR_D = 3.9     # component pins: thick collar then a thin pin
PIN_COLLAR_L = 9.0
BOSS_D_TOP = 10.4     # conical bosses beside the nav switch
BOSS_D_BOT = 7.6
BOSS_L = 6.9
BOSS_HOLE = 3.5

# plate outline (top view, mm); top surface at Z = 0
OUTLINE = [
    (0.0, 0.0),
    (92.0, 0.0),
    (184.9, -13.06),
    (184.9, -109.75),
    (115.8, -109.75),
    (115.8, -124.7),
    (65.0, -124.7),
    (26.0, -147.2),
    (0.0, -102.2),
]
# (corner, radius) for rounded vertical edges
CORNER_R = [((184.9, -13.06), 5.0), ((184.9, -109.75), 4.5), ((115.8, -109.75), 4.5),
            ((115.8, -124.7), STANDOFF_D / 2), ((26.0, -147.2), 5.0)]

# key columns: x centre, y of top key, number of keys
COL0_X = 70.0
COL_STAGGER = [-30.5, -28.4, -25.9, -28.4, -33.0, -33.0]   # y of the top key of each column
COL_KEYS = [5, 4, 4, 4, 4, 4]
COLS = [(COL0_X + i * COL_PITCH, y, n) for i, (y, n) in enumerate(zip(COL_STAGGER, COL_KEYS))]
EXTRA_KEYS = [(COL0_X + COL_PITCH, -106.7)]   # bottom-row key of column 1
THUMB_ANGLE = 30.0
THUMB_BASE = (31.1, -122.3)             # lower-left thumb key
THUMB_OFFS = [(0.0, 0.0), (PITCH, 0.0), (PITCH / 2, PITCH), (1.5 * PITCH, PITCH)]

# big square cut-out (display / sensor) and cross cut-out (nav switch)
SQ_C = (27.3, -23.3)
SQ_OUT = 29.2      # opening at the top surface (chamfered corners)
SQ_CH = 5.1
SQ_IN = 27.6       # through opening, leaving a ledge and four round screw pads
SQ_PAD_D = 4.6
SQ_HOLE_OFF = 11.85
SQ_HOLE_D = 2.0
SQ_CB_D = 3.2      # counterbore of the screw holes
SQ_CB_DEPTH = 0.35
CROSS_C = (41.8, -57.0)
CROSS_W = 29.0     # horizontal bar length
CROSS_H = 19.6     # horizontal bar height
CROSS_VW = 14.2    # vertical bar width
CROSS_VH = 32.9    # vertical bar length
STEP_D = 0.5       # depth of the ledge around the square and cross cut-outs

STANDOFFS = [(108.6, -117.4), (178.0, -103.0), (178.0, -19.2),
             (7.0, -6.8), (91.4, -6.7), (7.0, -100.5)]
COLLAR_PINS = [(5.0, -18.2), (3.6, -28.9),                  # square module
               (31.8, -44.4), (51.8, -44.0), (52.8, -70.6)]  # nav switch
PLAIN_PINS = [(3.9, -40.2, 15.0), (34.7, -72.8, 13.3), (3.3, -77.6, POST_L)]   # x, y, depth
BOSSES = [(16.2, -63.4), (15.7, -51.4)]
SIDE_TAB = (0.0, 2.5, -61.0, -48.5, 8.0)   # x0, x1, y0, y1, depth


# ---------------------------------------------------------------- helpers
def rot(p, ang):
    a = math.radians(ang)
    return (p[0] * math.cos(a) - p[1] * math.sin(a), p[0] * math.sin(a) + p[1] * math.cos(a))


def key_list():
    keys = []
    for x, y0, n in COLS:
        for i in range(n):
            keys.append((x, y0 - i * PITCH, 0.0))
    for x, y in EXTRA_KEYS:
        keys.append((x, y, 0.0))
    for ox, oy in THUMB_OFFS:
        d = rot((ox, oy), THUMB_ANGLE)
        keys.append((THUMB_BASE[0] + d[0], THUMB_BASE[1] + d[1], THUMB_ANGLE))
    return keys


def key_corner(k, sx, sy):
    x, y, a = k
    d = rot((sx * PITCH / 2, sy * PITCH / 2), a)
    return (x + d[0], y + d[1])


def square_solid(cx, cy, ang, size, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(cx, cy).transformed(rotate=(0, 0, ang))
            .rect(size, size).extrude(z1 - z0).val())


def cyl(cx, cy, d, z0, z1):
    return cq.Workplane("XY").workplane(offset=z0).center(cx, cy).circle(d / 2).extrude(z1 - z0).val()


def hull2(c1, r1, c2, r2, z0, z1):
    """Solid hull of two vertical cylinders (a web between two posts)."""
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dy)
    ux, uy = dx / d, dy / d
    nx, ny = -uy, ux
    s = (r1 - r2) / d
    c = math.sqrt(max(0.0, 1 - s * s))
    ma = (nx * c + ux * s, ny * c + uy * s)
    mb = (-nx * c + ux * s, -ny * c + uy * s)
    p1a = (c1[0] + r1 * ma[0], c1[1] + r1 * ma[1])
    p2a = (c2[0] + r2 * ma[0], c2[1] + r2 * ma[1])
    p2b = (c2[0] + r2 * mb[0], c2[1] + r2 * mb[1])
    p1b = (c1[0] + r1 * mb[0], c1[1] + r1 * mb[1])
    m2 = (c2[0] + r2 * ux, c2[1] + r2 * uy)
    m1 = (c1[0] - r1 * ux, c1[1] - r1 * uy)
    w = (cq.Workplane("XY").workplane(offset=z0).moveTo(*p1a).lineTo(*p2a)
         .threePointArc(m2, p2b).lineTo(*p1b).threePointArc(m1, p1a).close())
    return w.extrude(z1 - z0).val()


def cross_solid(z0, z1, grow=0.0):
    cx, cy = CROSS_C
    a = (cq.Workplane("XY").workplane(offset=z0).center(cx, cy)
         .rect(CROSS_W + 2 * grow, CROSS_H + 2 * grow).extrude(z1 - z0).val())
    b = (cq.Workplane("XY").workplane(offset=z0).center(cx, cy)
         .rect(CROSS_VW + 2 * grow, CROSS_VH + 2 * grow).extrude(z1 - z0).val())
    return a.fuse(b).clean()


def chamfered_square(cx, cy, size, ch, z0, z1):
    h = size / 2
    pts = [(-h + ch, -h), (h - ch, -h), (h, -h + ch), (h, h - ch),
           (h - ch, h), (-h + ch, h), (-h, h - ch), (-h, -h + ch)]
    return (cq.Workplane("XY").workplane(offset=z0).center(cx, cy)
            .polyline(pts).close().extrude(z1 - z0).val())


# ---------------------------------------------------------------- plate
plate = cq.Workplane("XY").workplane(offset=-PLATE_T).polyline(OUTLINE).close().extrude(PLATE_T)
for (px, py), r in CORNER_R:
    plate = plate.edges("|Z").edges(
        cq.selectors.NearestToPointSelector((px, py, -PLATE_T / 2))).fillet(r)
plate = plate.faces("<Z").edges().fillet(EDGE_R_BOT)
plate_s = plate.val()

keys = key_list()
ZT = -PLATE_T + 0.01     # features start just inside the plate

# ---------------------------------------------------------------- ribs under the plate
grid_keys = [k for k in keys if k[2] == 0.0]      # the thumb keys have no ribs
outer = [square_solid(x, y, 0.0, PITCH + RIB_W, -RIB_D, ZT) for x, y, a in grid_keys]
inner = [square_solid(x, y, 0.0, PITCH - RIB_W, -RIB_D - 1, 0.5) for x, y, a in grid_keys]
ribs = outer[0].fuse(*outer[1:]).clean()
ribs = ribs.cut(*inner)

# ---------------------------------------------------------------- posts at the cell corners
corners = []
for k in keys:
    for sx, sy in ((-1, -1), (1, -1), (1, 1), (-1, 1)):
        p = key_corner(k, sx, sy)
        if all((p[0] - q[0]) ** 2 + (p[1] - q[1]) ** 2 > 1.0 for q in corners):
            corners.append(p)


def corner_index(p):
    return min(range(len(corners)), key=lambda i: (corners[i][0] - p[0]) ** 2 + (corners[i][1] - p[1]) ** 2)


# webs: staggered neighbours closer than HULL_GAP, plus the two outer ends of the offset thumb rows
pairs = []
for i, p in enumerate(corners):
    for j in range(i + 1, len(corners)):
        q = corners[j]
        if math.hypot(p[0] - q[0], p[1] - q[1]) < HULL_GAP:
            pairs.append((i, j))
tb = keys[-4:]   # BL, BR, TL, TR
for a, b in ((key_corner(tb[0], -1, 1), key_corner(tb[2], -1, -1)),
             (key_corner(tb[1], 1, 1), key_corner(tb[3], 1, -1))):
    pairs.append((corner_index(a), corner_index(b)))

# group the joined corners; only the lowest corner of a group keeps a full-length post
group = list(range(len(corners)))


def root(i):
    while group[i] != i:
        i = group[i]
    return i


for i, j in pairs:
    group[root(i)] = root(j)
members = {}
for i in range(len(corners)):
    members.setdefault(root(i), []).append(i)
full_post = set(min(m, key=lambda i: corners[i][1]) for m in members.values())

posts = [cyl(corners[i][0], corners[i][1], POST_D, -POST_L, ZT) for i in sorted(full_post)]
webs = [hull2(corners[i], POST_D / 2, corners[j], POST_D / 2, -WEB_L, ZT) for i, j in pairs]

# ---------------------------------------------------------------- standoffs, pins and bosses
stand = []
for sx, sy in STANDOFFS:
    s = cyl(sx, sy, STANDOFF_D, -STANDOFF_L, ZT)
    s = s.cut(cyl(sx, sy, STANDOFF_HOLE, -STANDOFF_L - 1, -STANDOFF_L + 6.0))
    stand.append(s)
# back-right standoff is tied to the neighbouring corner post
cr = key_corner((COLS[5][0], COLS[5][1], 0.0), 1, 1)
stand.append(hull2(STANDOFFS[2], STANDOFF_D / 2 - 0.05, cr, POST_D / 2, -STANDOFF_L, ZT))

pins = []
for px, py in COLLAR_PINS:
    pins.append(cyl(px, py, PIN_COLLAR_D, -PIN_COLLAR_L, ZT))
    pins.append(cyl(px, py, POST_D, -POST_L, -PIN_COLLAR_L + 0.01))
for px, py, pl in PLAIN_PINS:
    pins.append(cyl(px, py, POST_D + 0.2, -pl, ZT))
for bx, by in BOSSES:
    cone = cq.Solid.makeCone(BOSS_D_BOT / 2, BOSS_D_TOP / 2, BOSS_L + ZT, cq.Vector(bx, by, -BOSS_L), cq.Vector(0, 0, 1))
    pins.append(cone.cut(cyl(bx, by, BOSS_HOLE, -BOSS_L - 1, -PLATE_T - 1.5)))
x0, x1, y0, y1, dep = SIDE_TAB
pins.append(cq.Workplane("XY").box(x1 - x0, y1 - y0, dep - PLATE_T + 0.01, centered=False)
            .translate((x0, y0, -dep)).val())

body = plate_s.fuse(ribs, *posts, *webs, *stand, *pins)

# ---------------------------------------------------------------- cut-outs
holes = [square_solid(x, y, a, HOLE, -RIB_D - 2, 1.0) for x, y, a in keys]
body = body.cut(*holes)

# square opening: stepped, with four round screw pads in the corners
pad_pts = [(SQ_C[0] + sx * SQ_HOLE_OFF, SQ_C[1] + sy * SQ_HOLE_OFF) for sx in (-1, 1) for sy in (-1, 1)]
top_cut = chamfered_square(SQ_C[0], SQ_C[1], SQ_OUT, SQ_CH, -STEP_D, 1.0)
top_cut = top_cut.cut(*[cyl(px, py, SQ_PAD_D, -STEP_D - 1, 2.0) for px, py in pad_pts])
body = body.cut(top_cut)
body = body.cut(*[cyl(px, py, SQ_CB_D, -SQ_CB_DEPTH, 1.0) for px, py in pad_pts])
thru = cq.Workplane("XY").workplane(offset=-RIB_D - 2).center(*SQ_C).rect(SQ_IN, SQ_IN).extrude(RIB_D + 3).val()
thru = thru.cut(*[cyl(px, py, SQ_PAD_D, -RIB_D - 3, 2.0) for px, py in pad_pts])
body = body.cut(thru)
body = body.cut(*[cyl(px, py, SQ_HOLE_D, -RIB_D - 2, 1.0) for px, py in pad_pts])

# cross opening: stepped
body = body.cut(cross_solid(-STEP_D, 1.0, grow=0.0))
body = body.cut(cross_solid(-RIB_D - 2, 1.0, grow=-0.8))

result = cq.Workplane("XY").add(body)
